import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
HALF_W = 20.0        # half width across the side flats (X)
Y_BACK = 20.9        # back-most point (+Y)
Y_FRONT = -20.9      # front-most point (-Y)
R_FRONT = 25.0       # large radius of the front face
FRONT_HALF = 10.6    # half width of the front face (seam to side surface)
SEAM_OFFSET = 0.15   # tiny crease on the front centre line

H_RIM = 41.0         # height of the open rim (front / sides)
H_TOP = 53.5         # height of the raised back wall
SLOPE_Y0 = 7.4       # Y where the slanted wall end meets the rim
SLOPE_Y1 = 11.9      # Y where the slanted wall end meets the top

# cavity
CAV_HALF_W = 16.1    # half width of cavity
CAV_Y_BACK = 16.4    # inner face of back wall
CAV_R_BACK = 6.5     # inner back corner radius
LOBE_R = 8.7         # radius of the two front lobes
LOBE_Y = -6.5        # centre Y of lobes
BRIDGE_Y = -14.3     # flat bridge between the two lobes
FLOOR_Z = 3.0        # floor height of the cavity

# floor pad with two through holes
PAD_X0, PAD_X1 = -15.3, 13.5
PAD_Y0, PAD_Y1 = -6.4, 7.5
PAD_H = 1.5
PAD_R = 1.2
TONGUE_W = 1.0
TONGUE_Y0, TONGUE_Y1 = -2.4, 3.8
HOLE_D = 6.4
HOLE_XS = (-11.7, 9.8)
HOLE_Y = 0.5

# side pockets (slots in the inner side walls)
POCKET_DEPTH = 8.6
NOTCH_DEPTH = 1.2
L_NOTCH = (-19.3, -15.0, -7.2, 5.65)   # shallow step in the left rim
NOTCH_FLARE = 0.22                      # flare (dy/dx) of the notch ends
L_POCKET = (-18.3, -15.0, -3.7, 4.6)   # x0, x1, y0, y1 (open slot)
R_POCKET = (15.0, 18.4, -3.8, 4.85)
# snap window behind the left slot: an undercut in the outer skin, with a
# lip at the top and a ramped catch in the middle
UNDERCUT_X = -19.3     # outer face of the undercut
LIP_T = 0.8            # lip thickness (below the rim step)
CATCH_RAMP = 1.8       # vertical length of the catch ramp
CATCH_H = 1.8          # height of the vertical catch face
LEDGE_H = 6.0          # height of the ledges under the pockets
L_LEDGE_X = -15.4      # inner face of the left ledge
L_LEDGE_Y0, L_LEDGE_Y1 = -2.5, 3.9
R_LEDGE_X_MID = 14.66  # crest of the curved right ledge
R_LEDGE_X_END = 16.3
R_LEDGE_Y0, R_LEDGE_Y1 = -7.3, 9.9

# front cross hole
FRONT_HOLE_D = 8.0
FRONT_HOLE_Z = 9.1

# small ejector-pin marks on the bottom face
PIN_MARKS = [(5.3, -11.8), (-7.2, -11.5), (5.1, 11.8), (-7.2, 11.7)]
PIN_D = 0.8
PIN_DEPTH = 0.2

RIM_FILLET = 1.2
SLOPE_FILLET = 1.0
TOP_FILLET = 0.5


def outer_profile():
    """Closed outline of the body in the XY plane.

    Front: two arcs of a large radius meeting at a seam on the centre line.
    Sides + back: one smooth spline (flats at +-X, rounded back).
    """
    # each front half is an arc of radius R_FRONT whose centre is shifted a
    # hair towards the other side -> a barely visible crease on the centre line
    ox = -SEAM_OFFSET                            # centre x of the right half
    fc_y = Y_FRONT + math.sqrt(R_FRONT ** 2 - ox ** 2)
    tx = FRONT_HALF
    ty = fc_y - math.sqrt(R_FRONT ** 2 - (tx - ox) ** 2)
    a0 = math.atan2(Y_FRONT - fc_y, -ox)
    a1 = math.atan2(ty - fc_y, tx - ox)
    a_mid = 0.5 * (a0 + a1)
    mx = ox + R_FRONT * math.cos(a_mid)
    my = fc_y + R_FRONT * math.sin(a_mid)
    # tangent of the front arc at its right end (CCW direction)
    t_r = ((fc_y - ty) / R_FRONT, (tx - ox) / R_FRONT)
    t_l = ((fc_y - ty) / R_FRONT, -(tx - ox) / R_FRONT)

    a = HALF_W
    right = [(a - 2.4, -12.5), (a, -3.0), (a, 3.0),
             (a - 1.15, 10.15), (a - 6.0, 16.5)]
    back = [(0.0, Y_BACK)]
    left = [(-x, y) for (x, y) in reversed(right)]
    pts = right + back + left + [(-tx, ty)]

    wp = (
        cq.Workplane("XY")
        .moveTo(-tx, ty)
        .threePointArc((-mx, my), (0, Y_FRONT))
        .threePointArc((mx, my), (tx, ty))
        .spline(pts, tangents=[t_r, t_l], includeCurrent=True, scale=False)
        .close()
    )
    return wp


# ---------------- main body ----------------
body = outer_profile().extrude(H_TOP)

# cut away everything in front of the slanted plane above the rim,
# leaving only the raised back wall
k = (SLOPE_Y1 - SLOPE_Y0) / (H_TOP - H_RIM)
z_hi = H_TOP + 10
cutter = (
    cq.Workplane("YZ", origin=(-30, 0, 0))
    .polyline([(-40, H_RIM), (SLOPE_Y0, H_RIM),
               (SLOPE_Y0 + k * (z_hi - H_RIM), z_hi), (-40, z_hi)])
    .close()
    .extrude(60)
)
body = body.cut(cutter)

# round the outer rim edge
body = body.edges(
    cq.selectors.BoxSelector((-30, -30, H_RIM - 0.01), (30, SLOPE_Y0 - 0.02, H_RIM + 0.01))
).fillet(RIM_FILLET)
# small concave round where the slanted wall ends meet the rim
try:
    body = body.edges(
        cq.selectors.BoxSelector((-30, SLOPE_Y0 - 0.01, H_RIM - 0.01),
                                 (30, SLOPE_Y0 + 0.01, H_RIM + 0.01))
    ).fillet(SLOPE_FILLET)
except Exception:
    pass
# soften the top edge of the raised back wall
body = body.edges(
    cq.selectors.BoxSelector((-30, SLOPE_Y1 - 0.01, H_TOP - 0.01), (30, 30, H_TOP + 0.01))
).fillet(TOP_FILLET)

# ---------------- cavity ----------------
def cavity_profile(z0):
    """Cavity outline: smooth rounded back + two circular lobes at the front,
    joined by a short flat bridge on the centre line."""
    lobe_x = CAV_HALF_W - LOBE_R
    dy = LOBE_Y - BRIDGE_Y
    bx = lobe_x - math.sqrt(LOBE_R ** 2 - dy ** 2)       # bridge half width
    a = CAV_HALF_W
    c = CAV_R_BACK * (1 - math.cos(math.pi / 4))
    back = [(a, LOBE_Y + 0.5 * (CAV_Y_BACK - CAV_R_BACK - LOBE_Y)),
            (a - c, CAV_Y_BACK - c),
            (0.0, CAV_Y_BACK)]
    pts = back + [(-x, y) for (x, y) in reversed(back[:-1])] + [(-a, LOBE_Y)]
    # mid point of the left lobe arc, from (-a, LOBE_Y) to (-bx, BRIDGE_Y)
    a0 = math.pi
    a1 = math.atan2(BRIDGE_Y - LOBE_Y, lobe_x - bx) + 2 * math.pi
    am = 0.5 * (a0 + a1)
    lmx = -lobe_x + LOBE_R * math.cos(am)
    lmy = LOBE_Y + LOBE_R * math.sin(am)
    return (
        cq.Workplane("XY", origin=(0, 0, z0))
        .moveTo(a, LOBE_Y)
        .spline(pts, tangents=[(0, 1), (0, -1)], includeCurrent=True, scale=False)
        .threePointArc((lmx, lmy), (-bx, BRIDGE_Y))
        .lineTo(bx, BRIDGE_Y)
        .threePointArc((-lmx, lmy), (a, LOBE_Y))
        .close()
    )


cav_h = H_TOP + 5 - FLOOR_Z
cavity = cavity_profile(FLOOR_Z).extrude(cav_h)
body = body.cut(cavity)

# ---------------- floor pad + holes ----------------
pad = (
    cq.Workplane("XY", origin=(0, 0, FLOOR_Z))
    .center((PAD_X0 + PAD_X1) / 2, (PAD_Y0 + PAD_Y1) / 2)
    .rect(PAD_X1 - PAD_X0, PAD_Y1 - PAD_Y0)
    .extrude(PAD_H)
    .edges("|Z").fillet(PAD_R)
)
body = body.union(pad)
# small tongue on the right end of the pad
tongue = (
    cq.Workplane("XY", origin=(0, 0, FLOOR_Z))
    .center(PAD_X1 + TONGUE_W / 2 - 0.5, (TONGUE_Y0 + TONGUE_Y1) / 2)
    .rect(TONGUE_W + 1.0, TONGUE_Y1 - TONGUE_Y0)
    .extrude(PAD_H)
)
body = body.union(tongue)
holes = (
    cq.Workplane("XY", origin=(0, 0, -1))
    .pushPoints([(x, HOLE_Y) for x in HOLE_XS])
    .circle(HOLE_D / 2)
    .extrude(FLOOR_Z + PAD_H + 2)
)
body = body.cut(holes)

# ---------------- side pockets ----------------
# shallow, slightly flared step in the left rim
x0, x1, y0, y1 = L_NOTCH
fl = NOTCH_FLARE * (x1 - x0)
notch = (
    cq.Workplane("XY", origin=(0, 0, H_RIM - NOTCH_DEPTH))
    .polyline([(x0, y0), (x1, y0 - fl), (x1, y1 + fl), (x0, y1)])
    .close()
    .extrude(NOTCH_DEPTH + 1)
)
body = body.cut(notch)
# deep pockets
for (x0, x1, y0, y1) in (L_POCKET, R_POCKET):
    pk = (
        cq.Workplane("XY", origin=(0, 0, H_RIM - POCKET_DEPTH))
        .center((x0 + x1) / 2, (y0 + y1) / 2)
        .rect(x1 - x0, y1 - y0)
        .extrude(POCKET_DEPTH + 1)
    )
    body = body.cut(pk)

# snap window in the left slot: undercut the outer skin between the lip
# and the slot floor, then put back the ramped catch
z_floor = H_RIM - POCKET_DEPTH
z_lip = H_RIM - NOTCH_DEPTH - LIP_T
x_in = L_POCKET[0]
ly0, ly1 = L_POCKET[2], L_POCKET[3]
undercut = (
    cq.Workplane("XY", origin=(0, 0, z_floor))
    .center((UNDERCUT_X + x_in + 0.2) / 2, (ly0 + ly1) / 2)
    .rect(x_in + 0.2 - UNDERCUT_X, ly1 - ly0)
    .extrude(z_lip - z_floor)
)
body = body.cut(undercut)
cz_mid = z_lip - CATCH_RAMP
catch = (
    cq.Workplane("XZ", origin=(0, ly1, 0))
    .polyline([(UNDERCUT_X - 0.3, cz_mid - CATCH_H), (x_in, cz_mid - CATCH_H),
               (x_in, cz_mid), (UNDERCUT_X, z_lip), (UNDERCUT_X - 0.3, z_lip)])
    .close()
    .extrude(ly1 - ly0)
)
body = body.union(catch)

# ledges below the pockets, standing slightly proud of the cavity walls
z_ledge = H_RIM - POCKET_DEPTH
l_ledge = (
    cq.Workplane("XY", origin=(0, 0, z_ledge - LEDGE_H))
    .center((-CAV_HALF_W - 0.3 + L_LEDGE_X) / 2, (L_LEDGE_Y0 + L_LEDGE_Y1) / 2)
    .rect(L_LEDGE_X + CAV_HALF_W + 0.3, L_LEDGE_Y1 - L_LEDGE_Y0)
    .extrude(LEDGE_H)
    .edges("|Z and >X").fillet(0.4)
)
body = body.union(l_ledge)
r_ledge = (
    cq.Workplane("XY", origin=(0, 0, z_ledge - LEDGE_H))
    .moveTo(CAV_HALF_W + 0.6, R_LEDGE_Y1)
    .lineTo(R_LEDGE_X_END, R_LEDGE_Y1)
    .threePointArc((R_LEDGE_X_MID, (R_LEDGE_Y0 + R_LEDGE_Y1) / 2), (R_LEDGE_X_END, R_LEDGE_Y0))
    .lineTo(CAV_HALF_W + 0.6, R_LEDGE_Y0)
    .close()
    .extrude(LEDGE_H)
)
body = body.union(r_ledge)

# ---------------- front cross hole ----------------
fh = (
    cq.Workplane("XZ", origin=(0, -12.0, 0))
    .center(0, FRONT_HOLE_Z)
    .circle(FRONT_HOLE_D / 2)
    .extrude(12.0)
)
body = body.cut(fh)

# ---------------- ejector-pin marks on the underside ----------------
pins = (
    cq.Workplane("XY", origin=(0, 0, -0.5))
    .pushPoints(PIN_MARKS)
    .circle(PIN_D / 2)
    .extrude(0.5 + PIN_DEPTH)
)
body = body.cut(pins)

result = body
